import math
import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeChamfer

# ---------------- driving dimensions (mm) ----------------
W = 62.0          # body width along X (hinge axis direction)
R = 30.0          # dome radius (profile is a half cylinder around the hinge axis)
LR = 7.2          # rim extends this far behind the hinge axis (+Y)
RF = 14.5         # fillet radius where dome meets the flat end walls
T = 3.0           # wall thickness
CH_Y = 2.2        # rim outer chamfer, along the outside
CH_S = 2.2        # rim outer chamfer, across the wall

# plan-view rounding of the back corners of the rim tabs (elliptical)
EA = 13.0         # along X
EB = 6.5          # along Y

# side-wall relief (middle of both end walls cut back to the hinge plane)
ZC = 18.1         # half height of the relief at the hinge plane
Y1 = 1.3          # short flat before the slanted relief edge
SLOPE = 0.58      # dz/dy of the slanted relief edge

# hinge features
PIN_D = 10.5      # pin / shaft diameter
STUB_L = 2.0      # +X pin stub length
SHAFT_L = 3.0     # -X shaft length between body and flange
FL_D = 20.8       # flange / knuckle diameter
FL_T = 3.4        # flange thickness
PRONG_L = 8.8     # prong length
SLOT_W = 11.5     # slot width between prongs (snap opening)
BORE_D = 15.0     # bore of the snap-on knuckle

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- outer body ----------------
prof = (
    cq.Workplane("YZ")
    .moveTo(LR, -R)
    .lineTo(0, -R)
    .threePointArc((-R, 0), (0, R))
    .lineTo(LR, R)
    .close()
    .extrude(W / 2, both=True)
)


def _end_edges(sel):
    """edges between the end walls and the dome/top/bottom (not on the rim)"""
    out = []
    for e in sel.vals():
        bb = e.BoundingBox()
        on_end = abs(abs(bb.xmin) - W / 2) < 1e-3 and abs(abs(bb.xmax) - W / 2) < 1e-3
        is_rim = bb.ymin > LR - 1e-3
        if on_end and not is_rim:
            out.append(e)
    return out


body = prof.newObject(_end_edges(prof.edges())).fillet(RF)

# hollow it, open at the rim face
body = body.faces(">Y").shell(-T)

# relief of the end walls between the rim tabs (profile in the YZ plane)
y_far = LR + 2.0
z_far = ZC + SLOPE * (y_far - Y1)
relief_pts = [(0, -ZC), (Y1, -ZC), (y_far, -z_far), (y_far, z_far), (Y1, ZC), (0, ZC)]
for sx in (1, -1):
    x0 = sx * (W / 2 - RF - 1.0)   # covers the whole corner blend region
    cutter = (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .polyline(relief_pts)
        .close()
        .extrude(sx * (RF + 4))
    )
    body = body.cut(cutter)

# elliptical plan-view rounding of the back corners (cuts the rim tabs)
for sx in (1, -1):
    cx = sx * (W / 2 - EA)
    cy = LR - EB
    block = (
        cq.Workplane("XY")
        .center(sx * (W / 2 - EA / 2 + 1), LR - EB / 2 + 1)
        .rect(EA + 2, EB + 2)
        .extrude(2 * R + 4)
        .translate((0, 0, -R - 2))
    )
    keep = (
        cq.Workplane("XY")
        .center(cx, cy)
        .ellipse(EA, EB)
        .extrude(2 * R + 4)
        .translate((0, 0, -R - 2))
    )
    body = body.cut(block.cut(keep))

# outer chamfer along the rim and down the cut edges of the rim tabs
def _on_outer(p, tol=1e-3):
    """point lies on the outer skin behind the hinge plane"""
    x, y, z = abs(p.x), p.y, abs(p.z)
    if y < -1e-6:
        return False
    if x <= W / 2 - RF:
        return abs(z - R) < tol
    if z <= R - RF:
        return abs(x - W / 2) < tol
    return abs(math.hypot(x - (W / 2 - RF), z - (R - RF)) - RF) < tol


def _rim_chamfer(wp, d_ref, d_out):
    solid = wp.val()
    ref_faces = []
    for f in wp.faces().vals():
        bb = f.BoundingBox()
        is_rim = f.geomType() == "PLANE" and bb.ymin > LR - 1e-6
        is_cut = f.geomType() not in ("PLANE", "CYLINDER", "TORUS") and bb.ymin > 0.5
        if is_rim or is_cut:
            ref_faces.append(f)
    mk = BRepFilletAPI_MakeChamfer(solid.wrapped)
    done = []
    for f in ref_faces:
        for e in f.Edges():
            if any(e.isSame(o) for o in done):
                continue
            if _on_outer(e.positionAt(0.5)) and _on_outer(e.positionAt(0.25)):
                done.append(e)
                mk.Add(d_ref, d_out, e.wrapped, f.wrapped)
    mk.Build()
    return cq.Workplane("XY").newObject([cq.Solid(mk.Shape())])


body = _rim_chamfer(body, CH_S, CH_Y)

# ---------------- hinge features ----------------
# +X pin stub
stub = cq.Workplane("YZ", origin=(W / 2 - T, 0, 0)).circle(PIN_D / 2).extrude(T + STUB_L)
body = body.union(stub)

# -X shaft, flange and slotted knuckle
x_end = -W / 2
shaft = cq.Workplane("YZ", origin=(x_end + T, 0, 0)).circle(PIN_D / 2).extrude(-(T + SHAFT_L))
flange = cq.Workplane("YZ", origin=(x_end - SHAFT_L, 0, 0)).circle(FL_D / 2).extrude(-FL_T)
knuckle = (
    cq.Workplane("YZ", origin=(x_end - SHAFT_L - FL_T, 0, 0))
    .circle(FL_D / 2)
    .extrude(-PRONG_L)
)
slot = cq.Workplane("XY").box(PRONG_L + 1, FL_D + 2, SLOT_W).translate(
    (x_end - SHAFT_L - FL_T - PRONG_L / 2 - 0.5, 0, 0)
)
bore = (
    cq.Workplane("YZ", origin=(x_end - SHAFT_L - FL_T, 0, 0))
    .circle(BORE_D / 2)
    .extrude(-(PRONG_L + 1))
)
knuckle = knuckle.cut(slot).cut(bore)
body = body.union(shaft).union(flange)
# keep the flange / knuckle seam (separately made knuckle)
body = body.union(knuckle, clean=False)

result = body
